import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
H = 220.0          # front panel height (Z)
B = 157.0          # front panel width (X)
FP_T = 1.8         # front panel thickness
PANEL_RECESS = 0.15  # panel face sits this far behind the post faces
INSET_X = 1.5      # body inset from panel outline (sides)
INSET_Z = 0.7      # body inset from panel outline (top / bottom)
BODY_L = 213.0     # length from front face to rear wall (Y)
RW_T = 3.5         # rear wall thickness
RW_GROW = 0.4      # rear wall / back plate stand proud of the body outline
GAP = 21.4         # gap between rear wall and back plate
BP_T = 3.5         # back plate thickness
CONN_REAR = 16.6   # connector overhang behind back plate

P = 7.8            # front corner post width (beyond panel side)
PD = 13.6          # post depth (Y)
TAB_H = 9.0        # tab height above/below panel
TAB_IN = 1.8       # tab overlap onto panel
HOLE_D = 5.2       # tab hole diameter

SC_R = 20.0        # scallop radius
SC_PITCH = 44.0    # scallop pitch
SC_N = 5           # number of scallops per post
SC_CLEAR = -0.3    # scallop bottom just past the panel side (clean cut)

N_SLAT = 18        # side slats -> N_SLAT-1 grooves
GR_W = 3.4         # groove width
GR_D = 0.12        # groove depth

SEAM_W = 0.4       # front seam groove width
SEAM_D = 0.3       # front seam groove depth

CONN_W = 50.0      # connector width (X)
CONN_X = 38.0      # connector column offset from centre
CP_T = 3.7         # card plate thickness
CS_H = 10.0        # guide sandwich overall height
CS_T = 1.2         # guide plate thickness
SLOT_DEPTH = 0.6   # blind slot depth
DIAMOND = 4.6      # centre diamond size
SLOT_W = 2.0       # slot width in connector plates
SLOT_LX = 34.0     # slot length along X
SLOT_LY = 33.0     # cross slot length along Y
SLOT_Y = 235.0     # slot position (Y)
STUB_W = 11.0
STUB_D = 5.6
STUB_H = 3.5
STUB_IN = 3.0

pitch = H / N_SLAT
Y_RW0 = BODY_L
Y_RW1 = BODY_L + RW_T
Y_BP0 = Y_RW1 + GAP
Y_BP1 = Y_BP0 + BP_T
Y_END = Y_BP1 + CONN_REAR
BX = B / 2 - INSET_X       # half width of body behind the panel


def box(x0, x1, y0, y1, z0, z1):
    return (cq.Workplane("XY")
            .box(x1 - x0, y1 - y0, z1 - z0, centered=False)
            .translate((x0, y0, z0)))


def fuse_all(base, tools):
    shp = base.val().fuse(*[t.val() for t in tools]).clean()
    return cq.Workplane("XY").add(shp)


def cut_all(base, tools):
    shp = base.val().cut(*[t.val() for t in tools]).clean()
    return cq.Workplane("XY").add(shp)


# ---------------- main body ----------------
body = box(-BX, BX, FP_T - 0.01, BODY_L, INSET_Z, H - INSET_Z)

# side grooves (slats)
grooves = []
for k in range(1, N_SLAT):
    zc = k * pitch
    g = box(BX - GR_D, BX + 1, PD, BODY_L + 0.01, zc - GR_W / 2, zc + GR_W / 2)
    grooves += [g, g.mirror("YZ")]
body = cut_all(body, grooves)

# front panel, rear wall, back plate (full outline)
panel = box(-B / 2 - P, B / 2 + P, PANEL_RECESS, FP_T, 0, H)
for sx in (1, -1):
    for i in range(SC_N):
        zc = H / 2 + (i - (SC_N - 1) / 2) * SC_PITCH
        panel = panel.cut(cq.Workplane("XZ").center(sx * (B / 2 + SC_CLEAR + SC_R), zc)
                          .circle(SC_R).extrude(-(FP_T + 2)).translate((0, -1, 0)))
body = body.union(panel)
body = body.union(box(-BX - RW_GROW, BX + RW_GROW, Y_RW0, Y_RW1,
                      INSET_Z - RW_GROW, H - INSET_Z + RW_GROW))
body = body.union(box(-BX - RW_GROW, BX + RW_GROW, Y_BP0, Y_BP1,
                      INSET_Z - RW_GROW, H - INSET_Z + RW_GROW))

# front seams
for zc in (H / 2 - SC_PITCH, H / 2 + SC_PITCH):
    s = box(-B / 2 - P - 1, B / 2 + P + 1, -0.01, PANEL_RECESS + SEAM_D,
            zc - SEAM_W / 2, zc + SEAM_W / 2)
    body = body.cut(s)


# ---------------- front corner posts ----------------
SC_XC = B / 2 + SC_CLEAR + SC_R                       # scallop centre X
SC_Z = [H / 2 + (i - (SC_N - 1) / 2) * SC_PITCH for i in range(SC_N)]


def scallops(x_c, y0, y1):
    cut = None
    for zc in SC_Z:
        cyl = (cq.Workplane("XZ").center(x_c, zc).circle(SC_R)
               .extrude(-(y1 - y0)).translate((0, y0, 0)))
        cut = cyl if cut is None else cut.union(cyl)
    return cut


def make_post():
    y0 = PANEL_RECESS
    post = box(B / 2, B / 2 + P, y0, PD, -TAB_H, H + TAB_H)
    # fill between post and the (inset) body side
    post = post.union(box(BX - 0.01, B / 2 + 0.01, FP_T - 0.01, PD, INSET_Z, H - INSET_Z))
    # tabs overlap slightly onto the panel top / bottom
    post = post.union(box(B / 2 - TAB_IN, B / 2 + P, y0, PD, H, H + TAB_H))
    post = post.union(box(B / 2 - TAB_IN, B / 2 + P, y0, PD, -TAB_H, 0))
    # the bumps between scallops stand a hair proud of the panel face
    for i in range(SC_N - 1):
        post = post.union(box(B / 2, B / 2 + P, 0, y0 + 0.01, SC_Z[i], SC_Z[i + 1]))
    post = post.cut(scallops(SC_XC, -1, PD + 1))
    # mounting holes in tabs
    xh = B / 2 + (P - TAB_IN) / 2
    for zh in (H + TAB_H / 2, -TAB_H / 2):
        hole = (cq.Workplane("XZ").center(xh, zh).circle(HOLE_D / 2)
                .extrude(-(PD + 2)).translate((0, -1, 0)))
        post = post.cut(hole)
    return post


post_r = make_post()
body = body.union(post_r).union(post_r.mirror("YZ"))


# ---------------- connectors ----------------
def slot_tools(xc, zface, up, cross):
    """Blind slot pattern (long X slot, centre diamond, optional Y slot)
    sunk into a horizontal plate face at height zface; up=True for a top face."""
    z0 = zface - SLOT_DEPTH if up else zface - 1.0
    hgt = SLOT_DEPTH + 1.0
    wp = cq.Workplane("XY").workplane(offset=z0)
    d = DIAMOND / 2
    tools = [wp.center(xc, SLOT_Y).slot2D(SLOT_LX, SLOT_W, 0).extrude(hgt),
             wp.center(xc, SLOT_Y)
             .polyline([(d, 0), (0, d), (-d, 0), (0, -d)]).close().extrude(hgt)]
    if cross:
        tools.append(wp.center(xc, (Y_RW1 + Y_END) / 2 - 2.0)
                     .slot2D(SLOT_LY, SLOT_W, 90).extrude(hgt))
    return tools


plates, slots = [], []


def plate(xc, z0, z1, cross, top=True, bottom=False):
    plates.append(box(xc - CONN_W / 2, xc + CONN_W / 2, Y_RW1 - 0.01, Y_END, z0, z1))
    if top:
        slots.extend(slot_tools(xc, z1, True, cross))
    if bottom:
        slots.extend(slot_tools(xc, z0, False, cross))


for k in range(1, N_SLAT):
    zc = H - k * pitch
    xl, xr = -CONN_X, CONN_X
    # -X column: card plate on every pitch
    plate(xl, zc - CP_T / 2, zc + CP_T / 2, False, True, True)
    if k % 2 == 1:
        # both columns: card plate sandwiched between two thin guide plates
        plate(xr, zc - CP_T / 2, zc + CP_T / 2, False, False)
        for xc, cross in ((xr, True), (xl, False)):
            plate(xc, zc + CS_H / 2 - CS_T, zc + CS_H / 2, cross, True)
            plate(xc, zc - CS_H / 2, zc - CS_H / 2 + CS_T, cross, False, True)
        # side guide stubs in front of the back plate
        st = box(BX - STUB_IN - STUB_W, BX - STUB_IN, Y_BP0 - STUB_D, Y_BP0 + 0.01,
                 zc - STUB_H / 2, zc + STUB_H / 2)
        plates += [st, st.mirror("YZ")]

conn = cut_all(fuse_all(plates[0], plates[1:]), slots)
body = fuse_all(body, [conn])

result = body
